import math
import cadquery as cq

# ---------------------------------------------------------------- parameters
YC = 6.3            # symmetry plane of the palm body (Y)
XL = 3.9            # flat (-X) face of the body
XC = 36.9           # centre of the round (+X) end (lobe layout centre)
ZB = -27.45         # body bottom
ZT = 1.4            # body top
H = ZT - ZB

# top features
BORE_X = 29.6
CB_R = 16.0         # opening radius in the top plate
TOP_T = 3.0         # top plate thickness above the octagonal cavity
OCT_R = 18.0        # octagon cavity circumradius
OCT_FLOOR = -8.0
THRU_R = 7.7
SHELL_T = 3.5       # side wall thickness of the hollow palm
BOT_T = 3.0         # bottom plate thickness
CUP_T = 2.5         # wall thickness of the octagonal cup hanging under the top plate
CUP_BOT = -11.5     # underside of the cup floor

# lobes (finger knuckles)
LOBE_ZC = -16.0
LOBE_BV = 10.3      # vertical semi axis of the +X lobes
LOBE_BH = (8.0, 9.5, 8.0)   # horizontal semi axes (-, middle, +)
LOBE_AF = 17.5      # axial semi axis of the +X lobes
LOBE_RC = 34.5      # lobe centres on this radius about the body centre
LOBE_POS = (-34.4, 0.0, 34.4)   # polar position of the centres
LOBE_DIR = (-17.6, 0.0, 17.6)   # axis directions
SIDE_BV = 11.2
SIDE_BH = 10.2
SIDE_AF = 16.0
SIDE_TILT = 25.0
SIDE_X = 19.7
SIDE_Y = 28.5       # centre offset from YC
SLOT_W = 2.6
SLOT_H = 15.5
SLOT_D = 7.0
PIN_R = 1.0
PIN_FROM_TIP = 4.5

# rear bracket (wedge + inclined plate + box)
WEDGE_X0 = -14.83   # wedge toe at Z = ZB
SLOPE = math.radians(60.7)
PLATE_T = 2.0
PLATE_HW = 22.3
PANEL_T = 2.0
PANEL_HW = 10.5
BOX_HW = 12.8
BOX_U0, BOX_U1 = 6.1, 35.3
BOX_V1 = 16.6

# back wall on top of the body
WALL_T = 8.2
WALL_HW = 19.5
WALL_TOP = 21.8

# loose parts
CYL_C = (-73.2, -102.6)
CYL_R = 15.8
CYL_Z = (-27.35, -3.4)

SHAFT_Y, SHAFT_Z = 104.6, 20.5
SHAFT_X0, SHAFT_X1 = -75.4, -8.8
SHAFT_R = 2.45

VG_XY = (23.6, 111.2)
PIN_XY = (26.9, 87.4)

STRIP_C = (43.8, -88.0)
STRIP_R = 27.5
STRIP_T = 1.7
STRIP_Z = (-12.55, -6.25)
STRIP_SPAN = 50.0


def cyl(r, h, base, axis=(0, 0, 1)):
    return cq.Workplane("XY").add(
        cq.Solid.makeCylinder(r, h, cq.Vector(*base), cq.Vector(*axis)))


# ---------------------------------------------------------------- body
# plan outline: flat rear face plus one smooth styled curve (symmetric about YC)
OUTLINE_HALF = [(XL, 21.6), (4.5, 24.4), (7.2, 27.6), (13.5, 30.3), (24.0, 31.3),
                (36.0, 31.3), (47.0, 30.3), (56.0, 27.0), (62.5, 21.8), (66.8, 13.8)]
XR = 68.65
pts = ([(x, YC - y) for (x, y) in OUTLINE_HALF] + [(XR, YC)]
       + [(x, YC + y) for (x, y) in reversed(OUTLINE_HALF)])


def outline(z0, p=pts):
    return (cq.Workplane("XY", origin=(0, 0, z0))
            .spline(p, includeCurrent=False).close())


def inset(p, d):
    """points of a closed outline moved inward by d (normal from neighbours)"""
    out = []
    n = len(p)
    for i in range(n):
        x0, y0 = p[i - 1] if i > 0 else (p[0][0], p[0][1] + 1.0)
        x1, y1 = p[i + 1] if i < n - 1 else (p[-1][0], p[-1][1] - 1.0)
        tx, ty = x1 - x0, y1 - y0
        ln = math.hypot(tx, ty)
        nx, ny = -ty / ln, tx / ln          # inward (outline runs counter-clockwise)
        out.append((p[i][0] + d * nx, p[i][1] + d * ny))
    return out


body = outline(ZB).extrude(H)

# ---------------------------------------------------------------- lobes
def egg(af, bv, bh):
    """ellipsoidal knuckle along +X (centre at origin), elliptical section;
    the revolve seam is put underneath"""
    arc = cq.Edge.makeEllipse(af, bv, cq.Vector(0, 0, 0), cq.Vector(0, 1, 0),
                              cq.Vector(1, 0, 0), 0, 180)
    ax = cq.Edge.makeLine(cq.Vector(-af, 0, 0), cq.Vector(af, 0, 0))
    w = cq.Wire.assembleEdges([arc, ax])
    sol = cq.Solid.revolve(w, [], 360, cq.Vector(0, 0, 0), cq.Vector(1, 0, 0))
    if abs(bh - bv) > 1e-6:
        sol = sol.transformGeometry(
            cq.Matrix([[1, 0, 0, 0], [0, bh / bv, 0, 0], [0, 0, 1, 0]]))
    return cq.Workplane("XY").add(sol)


def lobe(af, bv, bh, cx, cy, ang):
    e = egg(af, bv, bh)
    slot = (cq.Workplane("XY").box(2 * SLOT_D, SLOT_W, SLOT_H)
            .edges("|Y").fillet(SLOT_W / 2 - 0.05).translate((af, 0, 0)))
    hole = cyl(PIN_R, 4 * bh, (af - PIN_FROM_TIP, -2 * bh, 0), (0, 1, 0))
    e = e.cut(slot).cut(hole)
    return e.rotate((0, 0, 0), (0, 0, 1), ang).translate((cx, cy, LOBE_ZC))


lobes = []
for pos, dr, bh in zip(LOBE_POS, LOBE_DIR, LOBE_BH):
    cx = XC + LOBE_RC * math.cos(math.radians(pos))
    cy = YC + LOBE_RC * math.sin(math.radians(pos))
    lobes.append(lobe(LOBE_AF, LOBE_BV, bh, cx, cy, dr))
for sgn in (-1, 1):
    ang = sgn * (90.0 - SIDE_TILT)
    lobes.append(lobe(SIDE_AF, SIDE_BV, SIDE_BH, SIDE_X, YC + sgn * SIDE_Y, ang))
for lb in lobes:
    body = body.union(lb)

# ---------------------------------------------------------------- rear bracket
eu = (math.cos(SLOPE), math.sin(SLOPE))        # along the slope (X, Z)
ev = (-math.sin(SLOPE), math.cos(SLOPE))       # outward normal (X, Z)
O = (WEDGE_X0, ZB)


def sp(u, v):
    return (O[0] + u * eu[0] + v * ev[0], O[1] + u * eu[1] + v * ev[1])


u_top = (XL - WEDGE_X0) / eu[0]
wedge = (cq.Workplane("XZ", origin=(0, YC + PLATE_HW, 0))
         .polyline([(XL, ZB), O, (XL, ZB + u_top * eu[1])]).close()
         .extrude(2 * PLATE_HW))
body = body.union(wedge)

# local frame of the inclined face: x = u (up the slope), y = Y, z = v (out)
slope_plane = cq.Plane(origin=(O[0], YC, O[1]),
                       xDir=(eu[0], 0, eu[1]),
                       normal=(ev[0], 0, ev[1]))
NSEL = cq.selectors.ParallelDirSelector(cq.Vector(ev[0], 0, ev[1]))

u_plate0, u_plate = -3.0, 46.0
plate = (cq.Workplane(slope_plane)
         .center((u_plate0 + u_plate) / 2, 0)
         .rect(u_plate - u_plate0, 2 * PLATE_HW).extrude(PLATE_T))
# keep the plate below the body top line at the body face
plate = plate.intersect(cq.Workplane("XY").box(200, 200, 200)
                        .translate((XL + 1.0 - 100, YC, ZB + 100)))
body = body.union(plate)

panel = (cq.Workplane(slope_plane).workplane(offset=PLATE_T)
         .center(20.5, 0).rect(35.0, 2 * PANEL_HW).extrude(PANEL_T)
         .edges(NSEL).fillet(2.0))
body = body.union(panel)

# servo box on the inclined plate: bent-sheet look (rounded upper corners),
# two holes through the side flanges and two sockets in the outer face
v0 = PLATE_T + PANEL_T
BEND_R = 3.6
ucb = (BOX_U0 + BOX_U1) / 2
box = (cq.Workplane(slope_plane).workplane(offset=v0)
       .center(ucb, 0)
       .rect(BOX_U1 - BOX_U0, 2 * BOX_HW).extrude(BOX_V1 - v0))
box = box.edges(NSEL).edges(">Z").fillet(BEND_R)
box = box.edges(NSEL).edges("<Z").fillet(1.0)
vmid = (v0 + BOX_V1) / 2
for u in (11.0, 29.5):
    x, z = sp(u, vmid)
    box = box.cut(cyl(1.6, 40, (x, YC - 20, z), (0, 1, 0)))
SOCK_D = 4.0
for du in (-6.8, 6.8):
    sock = (cq.Workplane(slope_plane).workplane(offset=BOX_V1 - SOCK_D)
            .center(ucb + du, 0).rect(10.5, 2 * BOX_HW - 5.0).extrude(SOCK_D + 1))
    keep = (cq.Workplane(slope_plane).workplane(offset=BOX_V1 - SOCK_D - 0.5)
            .center(ucb + du, 0).rect(10.5, 4.0).extrude(SOCK_D - 0.5))
    for dy in (-7.2, 7.2):
        keep = keep.union(cq.Workplane(slope_plane).workplane(offset=BOX_V1 - SOCK_D - 0.5)
                          .center(ucb + du, dy).rect(3.5, 3.5).extrude(SOCK_D - 0.5))
    box = box.cut(sock.cut(keep))
body = body.union(box)

# ---------------------------------------------------------------- back wall
wall = (cq.Workplane("XY", origin=(0, 0, ZT - 0.01))
        .center(XL + WALL_T / 2, YC).rect(WALL_T, 2 * WALL_HW)
        .extrude(WALL_TOP - WALL_T / 2 - ZT + 0.01))
wall = wall.union(cyl(WALL_T / 2, 2 * WALL_HW,
                      (XL + WALL_T / 2, YC - WALL_HW, WALL_TOP - WALL_T / 2), (0, 1, 0)))
notch = cyl(3.1, 30, (XL - 5, YC, WALL_TOP - 1.1), (1, 0, 0))
wall = wall.cut(notch)
body = body.union(wall)

# ---------------------------------------------------------------- hollow palm
cav = outline(ZB + BOT_T, inset(pts, SHELL_T)).extrude(H - BOT_T - TOP_T)
cup = (cq.Workplane("XY", origin=(BORE_X, YC, CUP_BOT))
       .transformed(rotate=(0, 0, 22.5))
       .polygon(8, 2 * (OCT_R + CUP_T)).extrude(ZT - TOP_T - CUP_BOT))
cav = cav.cut(cup)
body = body.cut(cav)

# ---------------------------------------------------------------- top cuts
top_open = cyl(CB_R, TOP_T + 2, (BORE_X, YC, ZT - TOP_T - 1))
body = body.cut(top_open)
octo = (cq.Workplane("XY", origin=(BORE_X, YC, OCT_FLOOR))
        .transformed(rotate=(0, 0, 22.5))
        .polygon(8, 2 * OCT_R).extrude(ZT - TOP_T - OCT_FLOOR))
body = body.cut(octo)
body = body.cut(cyl(THRU_R, 60, (BORE_X, YC, ZB - 5)))
for ang in (67.5, 112.5, 157.5, 202.5, 247.5, 292.5, 337.5):
    a = math.radians(ang)
    body = body.cut(cyl(0.9, 6, (BORE_X + 16.8 * math.cos(a), YC + 16.8 * math.sin(a),
                                 OCT_FLOOR - 4)))

# crescent pocket toward +X: annular sector about the bore axis with round ends
CR_IN, CR_OUT, CR_ANG, CR_D = 20.3, 32.0, 38.0, 1.8


def sector(r_in, r_out, ang, z0, h):
    a = math.radians(ang)
    pin_ = lambda r, t: (BORE_X + r * math.cos(t), YC + r * math.sin(t))
    w = (cq.Workplane("XY", origin=(0, 0, z0))
         .moveTo(*pin_(r_in, -a)).lineTo(*pin_(r_out, -a))
         .threePointArc(pin_(r_out, 0.0), pin_(r_out, a))
         .lineTo(*pin_(r_in, a))
         .threePointArc(pin_(r_in, 0.0), pin_(r_in, -a))
         .close().extrude(h))
    return w


cres = sector(CR_IN, CR_OUT, CR_ANG, ZT - CR_D, CR_D + 1)
rm = (CR_IN + CR_OUT) / 2
for sgn in (-1, 1):
    a = math.radians(sgn * CR_ANG)
    cres = cres.union(cyl((CR_OUT - CR_IN) / 2, CR_D + 1,
                          (BORE_X + rm * math.cos(a), YC + rm * math.sin(a), ZT - CR_D)))
    a2 = math.radians(sgn * (CR_ANG + 5.0))
    cres = cres.union(cyl(4.0, CR_D + 1, (BORE_X + 29.0 * math.cos(a2),
                                          YC + 29.0 * math.sin(a2), ZT - CR_D)))
body = body.cut(cres)
# deeper channel along the crescent, interrupted by a central bridge
chan = sector(22.6, 29.7, 34.0, ZT - 6.0, 7.0)
bridge = cq.Workplane("XY").box(8.0, 16.0, 20).translate((54.6, YC, ZT - 4.0 - 10))
body = body.cut(chan.cut(bridge))
body = body.cut(cyl(1.0, 8, (54.6, YC, ZT - 9)))

# small holes in the top face
for (hx, hy) in ((22.0, 23.0), (35.3, 23.4), (22.0, -23.0), (35.3, -23.4),
                 (13.7, 19.0), (13.7, -19.0)):
    body = body.cut(cyl(1.1, 8, (hx, YC + hy, ZT - 6)))

# side windows (through along Y)
for (zc, hh) in ((-6.6, 8.2), (-21.0, 6.4)):
    win = (cq.Workplane("XZ", origin=(0, YC + 50, 0))
           .center(42.2, zc).ellipse(12.5, hh / 2).extrude(100))
    # keep the floor under the octagonal cavity intact
    win = win.cut(cq.Workplane("XY", origin=(BORE_X, YC, CUP_BOT - 0.2))
                  .transformed(rotate=(0, 0, 22.5))
                  .polygon(8, 2 * (OCT_R + CUP_T) + 0.4).extrude(OCT_FLOOR - CUP_BOT + 0.2))
    body = body.cut(win)

# ---------------------------------------------------------------- loose parts
cylinder = cyl(CYL_R, CYL_Z[1] - CYL_Z[0], (CYL_C[0], CYL_C[1], CYL_Z[0]))


def star(r_out, r_in, n):
    """trapezoidal tooth outline of a small gear"""
    sp_ = []
    for i in range(n):
        a0 = 2 * math.pi * i / n
        d = 2 * math.pi / n
        for f, r in ((0.0, r_in), (0.18, r_out), (0.42, r_out), (0.6, r_in)):
            a = a0 + f * d
            sp_.append((r * math.cos(a), r * math.sin(a)))
    return sp_


def bevel(r_small, r_big, h, n, plane):
    s = 0.82
    w = (cq.Workplane(plane)
         .polyline(star(r_small, r_small * s, n)).close()
         .workplane(offset=h)
         .polyline(star(r_big, r_big * s, n)).close()
         .loft(ruled=True))
    return w


# shaft with collar and bevel gear (axis along X)
shaft = cyl(SHAFT_R, SHAFT_X1 - SHAFT_X0 + 0.2, (SHAFT_X0, SHAFT_Y, SHAFT_Z), (1, 0, 0))
shaft = shaft.faces("<X").chamfer(0.4)
shaft = shaft.union(cyl(3.6, 5.8, (SHAFT_X1 - 0.1, SHAFT_Y, SHAFT_Z), (1, 0, 0)))
gx_plane = cq.Plane(origin=(-3.1, SHAFT_Y, SHAFT_Z), xDir=(0, 1, 0), normal=(1, 0, 0))
shaft = shaft.union(bevel(4.4, 7.6, 5.3, 16, gx_plane))
gx_plane2 = cq.Plane(origin=(2.2, SHAFT_Y, SHAFT_Z), xDir=(0, 1, 0), normal=(1, 0, 0))
shaft = shaft.union(bevel(7.6, 5.4, 1.2, 16, gx_plane2))
shaft = shaft.cut(cyl(1.5, 3, (1.6, SHAFT_Y, SHAFT_Z), (1, 0, 0)))

# vertical bevel gear with hub and spigot
gz_plane = cq.Plane(origin=(VG_XY[0], VG_XY[1], 13.0), xDir=(1, 0, 0), normal=(0, 0, 1))
vgear = bevel(7.45, 5.3, 2.5, 16, gz_plane)
vgear = vgear.union(
    cq.Workplane("XY").add(cq.Solid.makeCone(3.6, 6.8, 3.6,
                                             cq.Vector(VG_XY[0], VG_XY[1], 9.4))))
vgear = vgear.union(cyl(3.4, 5.0, (VG_XY[0], VG_XY[1], 4.5)))
vgear = vgear.union(cyl(2.6, 6.1, (VG_XY[0], VG_XY[1], -1.5)))
vgear = vgear.cut(cyl(2.5, 3, (VG_XY[0], VG_XY[1], 13.8)))

# top-hat bushing
pin = cyl(2.9, 12.7, (PIN_XY[0], PIN_XY[1], -14.2))
pin = pin.union(cyl(3.8, 4.2, (PIN_XY[0], PIN_XY[1], -1.7)))
pin = pin.cut(cyl(3.0, 1.5, (PIN_XY[0], PIN_XY[1], 1.0)))

# curved perforated strap
a0, a1 = math.radians(-STRIP_SPAN), math.radians(STRIP_SPAN)
ro, ri = STRIP_R + STRIP_T / 2, STRIP_R - STRIP_T / 2


def pol(r, a):
    return (STRIP_C[0] + r * math.cos(a), STRIP_C[1] + r * math.sin(a))


strip = (cq.Workplane("XY", origin=(0, 0, STRIP_Z[0]))
         .moveTo(*pol(ro, a0))
         .threePointArc(pol(ro, 0.0), pol(ro, a1))
         .lineTo(*pol(ri, a1))
         .threePointArc(pol(ri, 0.0), pol(ri, a0))
         .close()
         .extrude(STRIP_Z[1] - STRIP_Z[0]))
zmid = (STRIP_Z[0] + STRIP_Z[1]) / 2
for (ang, r) in ((-36.6, 0.6), (-17.6, 2.2), (-7.1, 0.6), (0.0, 0.6),
                 (8.9, 0.6), (21.6, 2.2), (40.2, 0.6)):
    a = math.radians(ang)
    d = (math.cos(a), math.sin(a), 0)
    p = (STRIP_C[0] + (STRIP_R - 3) * d[0], STRIP_C[1] + (STRIP_R - 3) * d[1], zmid)
    strip = strip.cut(cyl(r, 6, p, d))

result = (body.union(cylinder).union(shaft).union(vgear).union(pin).union(strip))
